import math
import cadquery as cq

# =====================================================================
#  Fork / yoke with an open-top box body.
#  X: from the fork tips (X=0) to the domed end of the box (X=XE)
#  Y: symmetric, Z: 0 = underside of the box, H = top rim of the box
# =====================================================================

# ---------------------------------------------------------------- box
H = 51.0            # box height (Z 0..H)
BX0 = 39.1          # box -X end face (bottom of the U opening)
XE = 100.2          # apex of the domed +X end face
BX1 = 95.7          # flat +X end of the box from which the dome protrudes
TOP_W = 11.6        # half width of the box at the top rim
MID_W = 13.2        # half width of the (slightly barrelled) box sides
MID_Z = 26.4        # height of the widest point of the box sides
BOT_W = 11.8        # half width where the side meets the rounded bottom
BOT_Z = 1.2         # height of that corner
BOT_FLAT = 7.0      # half width of the flat part of the underside
RIM_IN_W = 10.4     # inner half width of the open box
IN_X0 = 40.7        # inner face of the -X end wall
IN_X1 = 93.9        # inner face of the +X end wall
FLOOR_Z = 14.0      # inner floor of the open box
LEDGE_W = 10.1      # slightly narrower bottom of the inner pocket
LEDGE_H = 1.0
PAD_X = (47.0, 87.4)  # raised floor pads at both ends of the box interior
PAD_H = 1.5

END_RA = 21.2       # domed end face radius in plan (XY)
END_RB = 62.0       # domed end face radius in elevation (XZ), upper part
END_ZC = 25.0       # height of the most protruding point of the dome

# ---------------------------------------------------------------- arms
ARM_OUT = 36.9      # arm outer face |Y|
ARM_IN = 27.4       # arm inner face |Y|
S_XS = 24.5         # start of the outer S-curve (end of straight arm)
S_R1 = 24.0         # convex arc radius of the outer S-curve
S_R2 = 24.0         # concave arc radius of the outer S-curve
U_R = 12.5          # corner radius at the bottom of the U opening

TIP_R = 12.5        # rounded arm tip radius (front profile)
TIP_ZC = 25.0       # tip centre height
TOP_P = (34.5, 42.1)    # upper arm edge point before the root fillet
BOT_P = (35.5, 6.0)     # lower arm edge point before the root fillet
ROOT_R_TOP = 5.7
ROOT_R_BOT = 4.83

SIDE_SLOPE = 0.24   # slope of the arm top seen from the side
SIDE_P = (17.4, 47.4)
UNDER_SLOPE = 0.25  # slope of the arm underside seen from the side
UNDER_P = (17.4, 3.0)
SIDE_FR = 6.0       # concave blend of the arm top into the box rim

# ---------------------------------------------------------------- details
WIN_HW = 7.9        # end window half width
WIN_Z0 = 4.2
WIN_Z1 = 13.7
TUN_Z1 = 10.5       # through tunnel ceiling
WIN_DEPTH = 7.0

GROOVE_W = 2.0      # groove along the underside
GROOVE_D = 1.2
GROOVE_X0 = 47.0
SLOT_W = 4.8        # slot in the end face below the window
SLOT_X0 = 94.6      # depth of that slot

PIN_R = 6.2
PIN_H = 6.2
PIN_X = 76.5
PIN_FILLET = 1.6

SCREW_X = 76.4
SCREW_R = 6.4
HOLE_R = 1.45
HOLE_X = (44.1, 90.8)

POCKET_RC = (10.5, 25.3)   # round end centre of arm pocket (X, Z)
POCKET_R = 5.8
POCKET_X1 = 32.0           # flat end of arm pocket
POCKET_TOP1 = 26.1         # upper edge height at the flat end
POCKET_D0 = 4.0            # depth at the round end
POCKET_D1 = 1.0            # depth at the flat end

XEND = XE + 3.0


# ---------------------------------------------------------------- helpers
def arc_pts(c, r, a0, a1, n):
    return [(c[0] + r * math.cos(a0 + (a1 - a0) * i / n),
             c[1] + r * math.sin(a0 + (a1 - a0) * i / n)) for i in range(n + 1)]


def tangent_point(p, c, r, upper=True):
    """tangent point on circle (c, r) of a tangent line through p."""
    dx, dy = c[0] - p[0], c[1] - p[1]
    d = math.hypot(dx, dy)
    base = math.atan2(dy, dx)
    half = math.asin(r / d)
    ang = base - half if upper else base + half
    L = math.sqrt(d * d - r * r)
    return (p[0] + L * math.cos(ang), p[1] + L * math.sin(ang))


def root_fillet(p, t, xv, r, up=True):
    """fillet of radius r between line p-t and the vertical x = xv.
    returns centre, tangent point on the line and on the vertical."""
    dx, dy = p[0] - t[0], p[1] - t[1]
    L = math.hypot(dx, dy)
    ux, uy = dx / L, dy / L
    nx, ny = -uy, ux
    if (up and ny < 0) or ((not up) and ny > 0):
        nx, ny = -nx, -ny
    cx = xv - r
    cy = p[1] + (r - (cx - p[0]) * nx) / ny
    s = (cx - p[0]) * ux + (cy - p[1]) * uy
    a = (p[0] + s * ux, p[1] + s * uy)
    return (cx, cy), a, (xv, cy)


def lerp(a, b, t):
    return (a[0] + (b[0] - a[0]) * t, a[1] + (b[1] - a[1]) * t)


def seg_line(p0, p1, step=6.0):
    """points + unit tangents along a straight segment (end point excluded)."""
    n = max(1, round(math.dist(p0, p1) / step))
    d = ((p1[0] - p0[0]) / math.dist(p0, p1), (p1[1] - p0[1]) / math.dist(p0, p1))
    return [(lerp(p0, p1, i / n), d) for i in range(n)]


def seg_arc(c, r, a0, a1, step=5.0):
    """points + unit tangents along an arc from angle a0 to a1 (end excluded)."""
    n = max(2, round(abs(a1 - a0) * r / step))
    sgn = 1.0 if a1 > a0 else -1.0
    out = []
    for i in range(n):
        a = a0 + (a1 - a0) * i / n
        out.append(((c[0] + r * math.cos(a), c[1] + r * math.sin(a)),
                    (-sgn * math.sin(a), sgn * math.cos(a))))
    return out


def finish(segs, p_end, t_end):
    pts = [p for p, _ in segs] + [p_end]
    tans = [t for _, t in segs] + [t_end]
    return pts, tans


def rev(pts, tans):
    return pts[::-1], [(-t[0], -t[1]) for t in tans[::-1]]


def mir(pts, tans):
    return [(x, -y) for (x, y) in pts], [(t[0], -t[1]) for t in tans]


# ================================================================= arms
# ---- plan outline (XY) at three heights, lofted: the arms have vertical
#      outer faces while the box sides come out slightly barrelled
def outer_curves(yb):
    c1 = (S_XS, ARM_OUT - S_R1)
    dy = (ARM_OUT - S_R1) - (yb + S_R2)
    xe = S_XS + math.sqrt((S_R1 + S_R2) ** 2 - dy ** 2)
    c2 = (xe, yb + S_R2)
    k = S_R1 / (S_R1 + S_R2)
    t = (c1[0] + (c2[0] - c1[0]) * k, c1[1] + (c2[1] - c1[1]) * k)
    a1 = math.atan2(t[1] - c1[1], t[0] - c1[0])
    a2 = math.atan2(t[1] - c2[1], t[0] - c2[0])
    tan_t = (math.sin(a1), -math.cos(a1))
    # straight part + convex arc, up to the inflection t
    s1 = seg_line((0.0, ARM_OUT), (S_XS, ARM_OUT)) + seg_arc(c1, S_R1, math.pi / 2, a1)
    # concave arc running tangentially into the box side
    s2 = seg_arc(c2, S_R2, a2, -math.pi / 2) + seg_line((xe, yb), (XEND, yb), 8.0)
    return finish(s1, t, tan_t), finish(s2, (XEND, yb), (1.0, 0.0))


def inner_curve():
    c = (BX0 - U_R, ARM_IN - U_R)
    s = seg_line((0.0, ARM_IN), (c[0], ARM_IN)) + seg_arc(c, U_R, math.pi / 2, 0.0)
    return finish(s, (BX0, c[1]), (0.0, -1.0))


ic, ict = inner_curve()


def plan_wire(z, yb):
    (o1, o1t), (o2, o2t) = outer_curves(yb)
    w = cq.Workplane("XY", origin=(0, 0, z)).moveTo(*o1[0])
    w = w.spline(o1[1:], tangents=o1t, includeCurrent=True)
    w = w.spline(o2[1:], tangents=o2t, includeCurrent=True)
    w = w.lineTo(o2[-1][0], -o2[-1][1])
    q, qt = rev(*mir(o2, o2t))
    w = w.spline(q[1:], tangents=qt, includeCurrent=True)
    q, qt = rev(*mir(o1, o1t))
    w = w.spline(q[1:], tangents=qt, includeCurrent=True)
    w = w.lineTo(0, -ARM_IN)
    q, qt = mir(ic, ict)
    w = w.spline(q[1:], tangents=qt, includeCurrent=True)
    w = w.lineTo(*ic[-1])
    q, qt = rev(ic, ict)
    w = w.spline(q[1:], tangents=qt, includeCurrent=True)
    return w.close().val()


def barrel_w(z):
    """half width of the barrelled box side at height z (circle through 3 points)."""
    (y1, z1), (y2, z2), (y3, z3) = (BOT_W, BOT_Z), (MID_W, MID_Z), (TOP_W, H)
    a = [[2 * (y2 - y1), 2 * (z2 - z1)], [2 * (y3 - y1), 2 * (z3 - z1)]]
    b = [y2 ** 2 - y1 ** 2 + z2 ** 2 - z1 ** 2, y3 ** 2 - y1 ** 2 + z3 ** 2 - z1 ** 2]
    det = a[0][0] * a[1][1] - a[0][1] * a[1][0]
    yc = (b[0] * a[1][1] - b[1] * a[0][1]) / det
    zc = (a[0][0] * b[1] - a[1][0] * b[0]) / det
    r = math.hypot(y1 - yc, z1 - zc)
    return yc + math.sqrt(r * r - (z - zc) ** 2)


plan = cq.Workplane("XY").add(
    cq.Solid.makeLoft([plan_wire(-1.0, barrel_w(-1.0)), plan_wire(MID_Z, MID_W),
                       plan_wire(H + 1.0, barrel_w(H + 1.0))], False)
)

# ---- front (XZ): rounded tip, edges rising toward the box, root fillets
tc = (TIP_R, TIP_ZC)
tt = tangent_point(TOP_P, tc, TIP_R, upper=True)
tb = tangent_point(BOT_P, tc, TIP_R, upper=False)
ftc, fta, ftb = root_fillet(TOP_P, tt, BX0, ROOT_R_TOP, up=True)
fbc, fba, fbb = root_fillet(BOT_P, tb, BX0, ROOT_R_BOT, up=False)
ang_tt = math.atan2(tt[1] - tc[1], tt[0] - tc[0])
ang_tb = math.atan2(tb[1] - tc[1], tb[0] - tc[0])
ang_fba = math.atan2(fba[1] - fbc[1], fba[0] - fbc[0])
ang_fta = math.atan2(fta[1] - ftc[1], fta[0] - ftc[0])


def tip_outline():
    """bottom edge -> round tip -> top edge with tangents, for one spline."""
    a0 = ang_tb
    a1 = ang_tb - (2 * math.pi - (ang_tt - ang_tb))
    s = seg_line(fba, tb, 5.0) + seg_arc(tc, TIP_R, a0, a1, 4.0) + seg_line(tt, fta, 5.0)
    d = ((fta[0] - tt[0]) / math.dist(tt, fta), (fta[1] - tt[1]) / math.dist(tt, fta))
    return finish(s, fta, d)


tip_pts, tip_tan = tip_outline()
mid_fb = arc_pts(fbc, ROOT_R_BOT, 0.0, ang_fba, 2)[1]
mid_ft = arc_pts(ftc, ROOT_R_TOP, ang_fta, 0.0, 2)[1]

front = (
    cq.Workplane("XZ")
    .moveTo(BX0, H + 1)
    .lineTo(XEND, H + 1)
    .lineTo(XEND, -1)
    .lineTo(BX0, -1)
    .lineTo(*fbb)
    .threePointArc(mid_fb, fba)
    .spline(tip_pts[1:], tangents=tip_tan, includeCurrent=True)
    .threePointArc(mid_ft, ftb)
    .close()
    .extrude(60, both=True)
)


# ---- side (YZ): arm top / bottom slope gently outward, blending up to the rim
def side_curve():
    a = math.atan(SIDE_SLOPE)
    r = SIDE_FR
    zl = lambda y: SIDE_P[1] - SIDE_SLOPE * (y - SIDE_P[0])

    def centre(yt):
        return yt + r * math.sin(a), zl(yt) + r * math.cos(a)

    # find tangent point so that the concave blend passes through (TOP_W, H)
    lo, hi = TOP_W, TOP_W + 3 * r
    for _ in range(80):
        mid = 0.5 * (lo + hi)
        cy, cz = centre(mid)
        f = math.hypot(cy - TOP_W, cz - H) - r
        if f > 0:
            hi = mid
        else:
            lo = mid
    yt = 0.5 * (lo + hi)
    cy, cz = centre(yt)
    ang_h = math.atan2(H - cz, TOP_W - cy)
    ang_t = math.atan2(zl(yt) - cz, yt - cy)
    yfar = 60.0
    s = seg_arc((cy, cz), r, ang_h, ang_t, 1.5) + seg_line((yt, zl(yt)), (yfar, zl(yfar)), 6.0)
    return finish(s, (yfar, zl(yfar)), (math.cos(a), -math.sin(a)))


sc, sct = side_curve()


def bottom_curve():
    """underside: flat, rounded box corner, then the gently rising arm underside."""
    r = ((BOT_W - BOT_FLAT) ** 2 + BOT_Z ** 2) / (2 * BOT_Z)
    c = (BOT_FLAT, r)
    a1 = math.atan2(BOT_Z - c[1], BOT_W - c[0])
    zb = lambda y: UNDER_P[1] + UNDER_SLOPE * (y - UNDER_P[0])
    a = math.atan(UNDER_SLOPE)
    s = seg_arc(c, r, -math.pi / 2, a1, 1.5)
    s.append(((BOT_W, BOT_Z), (-math.sin(a1), math.cos(a1))))
    s += seg_line((UNDER_P[0], zb(UNDER_P[0])), (60.0, zb(60.0)), 6.0)
    return finish(s, (60.0, zb(60.0)), (math.cos(a), math.sin(a)))


bc, bct = bottom_curve()


def neg(pts, tans):
    return [(-y, z) for (y, z) in pts], [(-t[0], t[1]) for t in tans]


side = cq.Workplane("YZ", origin=(-2, 0, 0)).moveTo(-sc[0][0], H).lineTo(*sc[0])
side = side.spline(sc[1:], tangents=sct, includeCurrent=True)
# whole underside as one smooth curve: right arm -> rounded corner -> flat -> left
q1, qt1 = rev(bc, bct)
q2, qt2 = neg(bc, bct)
q, qt = q1 + [(0.0, 0.0)] + q2, qt1 + [(-1.0, 0.0)] + qt2
side = side.lineTo(*q[0]).spline(q[1:], tangents=qt, includeCurrent=True)
q, qt = rev(*neg(sc, sct))
side = side.lineTo(*q[0]).spline(q[1:], tangents=qt, includeCurrent=True)
side = side.close().extrude(XEND + 5)

body = plan.intersect(front).intersect(side)

# ================================================================= domed end face
# flat box end at BX1 with a dome protruding from it; the dome is bounded by
# two crossing cylinders: curved in plan (END_RA) and in elevation (END_RB)
end_block = (
    cq.Workplane("XY")
    .box(XEND + 5 - BX1, 2 * END_RA + 10, H + 20, centered=(False, True, False))
    .translate((BX1, 0, -10))
)
cyl_a = cq.Workplane("XY").center(XE - END_RA, 0).circle(END_RA).extrude(H + 40).translate((0, 0, -20))
# elevation profile of the dome: circular arc above END_ZC, a fuller
# elliptical quarter below it that runs back to the flat end at the bottom
def dome_profile():
    ea, eb = XE - BX1, END_ZC        # ellipse semi axes (X, Z), centre (BX1, END_ZC)
    pts, tans = [], []
    n = 8
    for i in range(n + 1):
        t = -math.pi / 2 + (math.pi / 2) * i / n
        pts.append((BX1 + ea * math.cos(t), END_ZC + eb * math.sin(t)))
        d = (-ea * math.sin(t), eb * math.cos(t))
        L = math.hypot(*d)
        tans.append((d[0] / L, d[1] / L))
    return pts, tans


dp, dpt = dome_profile()
arc_c = (XE - END_RB, END_ZC)
z_top = H + 3.0
x_top = arc_c[0] + math.sqrt(END_RB ** 2 - (z_top - END_ZC) ** 2)
a_top = math.atan2(z_top - END_ZC, x_top - arc_c[0])
arc_mid = (arc_c[0] + END_RB * math.cos(a_top / 2), END_ZC + END_RB * math.sin(a_top / 2))
cyl_b = (
    cq.Workplane("XZ")
    .moveTo(BX1 - 10, -5)
    .lineTo(BX1, -5)
    .lineTo(*dp[0])
    .spline(dp[1:], tangents=dpt, includeCurrent=True)
    .threePointArc(arc_mid, (x_top, z_top))
    .lineTo(BX1 - 10, z_top)
    .close()
    .extrude(40, both=True)
)
body = body.cut(end_block.cut(cyl_a.intersect(cyl_b)))

# ================================================================= open box pocket
pocket = (
    cq.Workplane("XY", origin=(0, 0, FLOOR_Z + LEDGE_H))
    .center((IN_X0 + IN_X1) / 2, 0)
    .rect(IN_X1 - IN_X0, 2 * RIM_IN_W)
    .extrude(H)
)
pocket_low = (
    cq.Workplane("XY", origin=(0, 0, FLOOR_Z))
    .center((IN_X0 + IN_X1) / 2, 0)
    .rect(IN_X1 - IN_X0, 2 * LEDGE_W)
    .extrude(LEDGE_H + 0.5)
)
body = body.cut(pocket).cut(pocket_low)
# raised pads at both ends of the floor
pad_l = cq.Workplane("XY").box(PAD_X[0] - IN_X0 + 0.2, 2 * LEDGE_W + 0.2, PAD_H + 0.1, centered=(False, True, False)).translate((IN_X0 - 0.1, 0, FLOOR_Z - 0.1))
pad_r = cq.Workplane("XY").box(IN_X1 - PAD_X[1] + 0.2, 2 * LEDGE_W + 0.2, PAD_H + 0.1, centered=(False, True, False)).translate((PAD_X[1], 0, FLOOR_Z - 0.1))
body = body.union(pad_l).union(pad_r)

# tunnel along the bottom of the box and the window in the domed end
tunnel = (
    cq.Workplane("XY")
    .box(XEND + 10 - 30, 2 * WIN_HW, TUN_Z1 - WIN_Z0, centered=(False, True, False))
    .translate((30, 0, WIN_Z0))
)
window = (
    cq.Workplane("XY")
    .box(20, 2 * WIN_HW, WIN_Z1 - WIN_Z0, centered=(False, True, False))
    .translate((XE - WIN_DEPTH, 0, WIN_Z0))
)
body = body.cut(tunnel).cut(window)

# groove along the underside and slot in the end face below the window
groove = (
    cq.Workplane("XY")
    .box(XEND + 5 - GROOVE_X0, GROOVE_W, GROOVE_D + 0.1, centered=(False, True, False))
    .translate((GROOVE_X0, 0, -0.1))
)
slot = (
    cq.Workplane("XY")
    .box(XEND + 5 - SLOT_X0, SLOT_W, WIN_Z0 + 1, centered=(False, True, False))
    .translate((SLOT_X0, 0, -0.5))
)
body = body.cut(groove).cut(slot)


# ================================================================= ramped pockets on the arm inner faces
def arm_pocket(sign):
    c, r = POCKET_RC, POCKET_R
    top_pt = tangent_point((POCKET_X1, POCKET_TOP1), c, r, upper=True)
    z_bot = c[1] - r
    mid = (c[0] - r, c[1])
    outline = (
        cq.Workplane("XZ")
        .moveTo(POCKET_X1, z_bot)
        .lineTo(POCKET_X1, POCKET_TOP1)
        .lineTo(*top_pt)
        .threePointArc(mid, (c[0], z_bot))
        .close()
        .extrude(50, both=True)
    )
    # floor ramps from POCKET_D0 deep (round end) to POCKET_D1 (flat end)
    x0 = c[0] - r
    yd = lambda x: ARM_IN + POCKET_D0 + (POCKET_D1 - POCKET_D0) * (x - x0) / (POCKET_X1 - x0)
    ramp = (
        cq.Workplane("XY", origin=(0, 0, -5))
        .polyline([(x0 - 2, ARM_IN - 6), (x0 - 2, yd(x0 - 2)),
                   (POCKET_X1 + 2, yd(POCKET_X1 + 2)), (POCKET_X1 + 2, ARM_IN - 6)])
        .close()
        .extrude(60)
    )
    cutter = outline.intersect(ramp)
    if sign < 0:
        cutter = cutter.mirror("XZ")
    return cutter


body = body.cut(arm_pocket(1)).cut(arm_pocket(-1))

# ================================================================= pin under the box
pin = (
    cq.Workplane("XY", origin=(0, 0, 0.5))
    .center(PIN_X, 0)
    .circle(PIN_R)
    .extrude(-PIN_H - 0.5)
    .faces("<Z").edges()
    .fillet(PIN_FILLET)
)
body = body.union(pin)

# ================================================================= floor details: screw head and two holes
screw = (
    cq.Workplane("XY", origin=(0, 0, FLOOR_Z))
    .center(SCREW_X, 0)
    .circle(SCREW_R)
    .extrude(1.5)
)
screw_slot = (
    cq.Workplane("XY")
    .box(2 * SCREW_R + 2, 1.2, 1.0, centered=(True, True, False))
    .translate((SCREW_X, 0, FLOOR_Z + 0.8))
)
body = body.union(screw).cut(screw_slot)
holes = (
    cq.Workplane("XY", origin=(0, 0, FLOOR_Z + PAD_H + 3))
    .pushPoints([(x, 0) for x in HOLE_X])
    .circle(HOLE_R)
    .extrude(-6)
)
body = body.cut(holes)

# keep a single clean solid
_solids = body.solids().vals()
if len(_solids) > 1:
    body = cq.Workplane("XY").add(max(_solids, key=lambda s: s.Volume()))

result = body
